import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 64.5          # overall width  (X)
H = 100.0         # overall height (Z)
D = 44.0          # overall depth  (Y), front face at y=0, open back at y=D
R_EDGE = 4.7      # fillet radius of the four edges running front-to-back
T = 2.6           # wall thickness

# top slot (through the top wall)
SLOT_L = 38.6
SLOT_W = 2.7
SLOT_X = 1.65              # slot centre offset in X
SLOT_Y = 25.2              # slot centre from the front face

# round holes, same position in both side walls
HOLE_D = 12.7
HOLE_Y = 12.8              # from front face
HOLE_Z = 68.5              # from bottom

# obround slot in the -X wall, below the hole
OB_L = 14.5
OB_W = 5.0
OB_Y = 14.3               # from front face
OB_Z = 37.0
OB_CH = 1.2                # countersink chamfer

# square hole in the bottom wall
SQ = 5.6
SQ_X = 2.4
SQ_Y = 17.3

# snap bumps on the inner faces of both side walls
BUMP_R = 2.4
BUMP_Y = 35.0
BUMP_Z = (21.0, 79.0)

# guide tabs hanging from the top wall at the slot ends
TAB_XIN = (17.8, -14.1)    # inner faces of the tabs (towards the slot centre)
TAB_TX = 3.6               # tab thickness in X
TAB_Y0 = 22.5              # front face of the tabs (they straddle the slot)
TAB_Y1 = (33.5, 26.6)      # back face of each tab
TAB_ZB = 71.0              # lower end of the tabs
TAB_RAMP = 3.5             # depth of the lead-in ramp seen through the slot

# back plate hanging from the top wall behind the slot
PLATE_Y0, PLATE_Y1 = 26.6, 29.5
PLATE_ZB = 75.5

# guide blocks standing on the floor (with a ramp towards the front)
BLK_X = (12.8, -11.95)
BLK_TX = 3.6
BLK_Y0 = 18.0
BLK_Y1 = (26.8, 24.0)
BLK_H = 8.8
RAMP_L = 5.0

# small clips hanging from the top wall just below the slot
CLIP_X = ((11.0, 14.6), (-13.6, -10.3))
CLIP_Y0, CLIP_Y1 = 22.5, 26.6
CLIP_H = 9.0

# small ribs on the inner face of the front wall
RIB_X = (12.8, -11.95)
RIB_TX = 3.6
RIB_DY = 3.4
RIB_H = 8.0

# thickening pads on the inner faces of the side walls
PAD_T = 4.0               # thickness at the front wall
PAD_Y1 = 17.0             # wedge runs out on the side wall here
PAD_Z0, PAD_Z1 = 15.0, 57.3

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- outer shell ----------------
outer = (
    cq.Workplane("XZ")
    .center(0, H / 2)
    .rect(W, H)
    .extrude(-D)                       # XZ normal is -Y, so -D extrudes towards +Y
    .edges("|Y")
    .fillet(R_EDGE)
)

cavity = (
    cq.Workplane("XZ", origin=(0, T, 0))
    .center(0, H / 2)
    .rect(W - 2 * T, H - 2 * T)
    .extrude(-(D - T + 1))
    .edges("|Y")
    .fillet(R_EDGE - T)
)

body = outer.cut(cavity)

# ---------------- internal features ----------------
xi = W / 2 - T      # inner face of the side walls
zt = H - T          # underside of the top wall

def block(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


# guide tabs under the top wall, with a lead-in ramp below the slot ends
slot_x0 = SLOT_X - SLOT_L / 2
slot_x1 = SLOT_X + SLOT_L / 2
for xin, ty1 in zip(TAB_XIN, TAB_Y1):
    sgn = 1 if xin > 0 else -1
    xout = xin + sgn * TAB_TX
    tab = block(min(xin, xout), max(xin, xout), TAB_Y0, ty1, TAB_ZB, zt + 0.5)
    xend = slot_x1 if sgn > 0 else slot_x0
    ramp_cut = (
        cq.Workplane("XZ", origin=(0, SLOT_Y - SLOT_W / 2, 0))
        .polyline([(xin - sgn * 0.5, zt + 1), (xend, zt + 1), (xend, zt), (xin, zt - TAB_RAMP), (xin - sgn * 0.5, zt - TAB_RAMP)])
        .close()
        .extrude(-SLOT_W)
    )
    tab = tab.cut(ramp_cut)
    body = body.union(tab)

# back plate behind the slot, from the +X tab to the -X side wall
body = body.union(block(-xi - 0.5, TAB_XIN[0], PLATE_Y0, PLATE_Y1, PLATE_ZB, zt + 0.5))

# guide blocks on the floor with a lead-in ramp towards the front
for bx, by1 in zip(BLK_X, BLK_Y1):
    ramp = (
        cq.Workplane("YZ", origin=(bx - BLK_TX / 2, 0, 0))
        .polyline([
            (BLK_Y0 - RAMP_L, T - 0.5),
            (by1, T - 0.5),
            (by1, T + BLK_H),
            (BLK_Y0, T + BLK_H),
        ])
        .close()
        .extrude(BLK_TX)
    )
    body = body.union(ramp)

# clips under the top wall
for cx0, cx1 in CLIP_X:
    body = body.union(block(cx0, cx1, CLIP_Y0, CLIP_Y1, zt - CLIP_H, zt + 0.5))

# ribs on the inner front wall
for rx in RIB_X:
    body = body.union(block(rx - RIB_TX / 2, rx + RIB_TX / 2, T - 0.5, T + RIB_DY, T - 0.5, T + RIB_H))

# cove-shaped thickening pads on both side walls: 4 mm thick at the front wall,
# running out tangentially into the side wall towards the open back
dy_pad = PAD_Y1 - T
r_cove = (PAD_T ** 2 + dy_pad ** 2) / (2 * PAD_T)       # arc tangent to the side wall
a_mid = 0.5 * math.asin(dy_pad / r_cove)
for sx in (1, -1):
    mid = (sx * (xi - r_cove * (1 - math.cos(a_mid))), PAD_Y1 - r_cove * math.sin(a_mid))
    pad = (
        cq.Workplane("XY", origin=(0, 0, PAD_Z0))
        .moveTo(sx * (xi + 0.5), T - 0.5)
        .lineTo(sx * (xi - PAD_T), T - 0.5)
        .lineTo(sx * (xi - PAD_T), T)
        .threePointArc(mid, (sx * xi, PAD_Y1))
        .lineTo(sx * (xi + 0.5), PAD_Y1)
        .close()
        .extrude(PAD_Z1 - PAD_Z0)
    )
    body = body.union(pad)

# snap bumps on both inner side walls
for sx in (1, -1):
    for bz in BUMP_Z:
        bump = cq.Workplane("YZ").sphere(BUMP_R).translate((sx * xi, BUMP_Y, bz))
        body = body.union(bump)

# ---------------- cut-outs ----------------
# top slot
slot = (
    cq.Workplane("XY", origin=(SLOT_X, SLOT_Y, H - T - 1))
    .rect(SLOT_L, SLOT_W)
    .extrude(T + 2)
)
body = body.cut(slot)

# side holes through both side walls
hole = (
    cq.Workplane("YZ", origin=(-W, HOLE_Y, HOLE_Z))
    .circle(HOLE_D / 2)
    .extrude(2 * W)
)
body = body.cut(hole)

# obround slot with countersink in the -X wall
ob = (
    cq.Workplane("YZ", origin=(-W / 2 - 1, OB_Y, OB_Z))
    .slot2D(OB_L, OB_W, angle=90)
    .extrude(T + PAD_T + 2)
)
body = body.cut(ob)
csk = (
    cq.Workplane("YZ", origin=(-W / 2 - 0.01, OB_Y, OB_Z))
    .slot2D(OB_L + 2 * OB_CH, OB_W + 2 * OB_CH, angle=90)
    .extrude(OB_CH, taper=45)
)
body = body.cut(csk)

# square hole in the bottom
sq = (
    cq.Workplane("XY", origin=(SQ_X, SQ_Y, -1))
    .rect(SQ, SQ)
    .extrude(T + 2)
)
body = body.cut(sq)

result = body
